import cadquery as cq

# ---------------- Driving dimensions (mm) ----------------
OD = 40.0          # outer diameter of the bushing
ID = 28.0          # bore diameter
H = 30.6           # overall height (axis along Z)
R_OUT = 1.0        # fillet on the outer rim edges (top & bottom)
R_IN = 1.1         # fillet on the bore rim edges (top & bottom)

ro, ri = OD / 2.0, ID / 2.0

# Plain tube: annulus extruded along +Z
tube = (
    cq.Workplane("XY")
    .circle(ro)
    .circle(ri)
    .extrude(H)
)

# Round the outer rims
tube = (
    tube.edges("%CIRCLE")
    .filter(lambda e: abs(e.radius() - ro) < 1e-6)
    .fillet(R_OUT)
)
# Round the bore rims
tube = (
    tube.edges("%CIRCLE")
    .filter(lambda e: abs(e.radius() - ri) < 1e-6)
    .fillet(R_IN)
)

# Centre the part on the origin; turn the (cosmetic) cylinder seam to the back
result = tube.translate((0, 0, -H / 2.0)).rotate((0, 0, 0), (0, 0, 1), 45)

VIEW = {"azimuth": 45, "elevation": 26}
